import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
RING_OD = 60.0        # eye ring outer diameter
RING_ID = 40.0        # eye ring bore (upper part)
BORE2_D = 37.0        # smaller bore in the lower part of the ring
BORE2_H = 10.0        # height of the lower, smaller bore
RING_H = 30.0         # eye ring height (z 0..RING_H)
RING_FIL = 7.5        # fillet on ring bottom outer edge

ARM_W = 40.0          # arm width (Y)
ARM_Z0 = 10.0         # arm bottom height
ARM_Z1 = RING_H       # arm top height (flush with ring top)
ARM_END = 140.0       # arm end, measured from ring centre
ARM_BOT_FIL = 7.0     # fillet on arm bottom long edges
NECK_TOP_FIL = 8.0    # fillet on neck top long edges

HUMP_X0 = 50.0        # start of raised hump
HUMP_Z = 50.0         # hump top height
HUMP_FIL = 7.0        # hump top edge fillets
HUMP_VFIL = 7.0       # hump vertical step edges
STEP_FIL = 7.0        # concave fillet at foot of hump
SLOPE_X0 = 72.0       # slope starts (on hump top)
SLOPE_X1 = 130.0      # slope ends (at arm top level)

HOLE_D = 6.0          # holes perpendicular to slope
HOLE_X = (87.25, 115.75)
BOSS_D = 20.0         # bosses under the holes
BOSS_DEPTH = 35.0     # boss face distance below slope plane (along normal)

# ---------------- derived ----------------
slope = (HUMP_Z - ARM_Z1) / (SLOPE_X1 - SLOPE_X0)
theta = math.atan(slope)  # slope angle
# unit normal of slope plane (pointing up, towards +X)
nx, nz = math.sin(theta), math.cos(theta)


def z_slope(x):
    return HUMP_Z - (x - SLOPE_X0) * slope


def _near(e, p, tol=0.5):
    c = e.Center()
    return abs(c.x - p[0]) < tol and abs(c.y - p[1]) < tol and abs(c.z - p[2]) < tol


def multi_fillet(shape, specs):
    """Fillet several edges (picked by their centre point), each with its own
    radius, in one fillet operation (falls back to one edge group at a time)."""
    mk = BRepFilletAPI_MakeFillet(shape.wrapped)
    for e in shape.Edges():
        for p, r in specs:
            if _near(e, p):
                mk.Add(r, e.wrapped)
    mk.Build()
    if mk.IsDone():
        return cq.Shape.cast(mk.Shape())
    out = shape
    for p, r in specs:
        try:
            edges = [e for e in out.Edges() if _near(e, p)]
            if edges:
                out = out.fillet(r, edges)
        except Exception:
            pass
    return out


# ---------------- eye ring ----------------
ring = (
    cq.Workplane("XY")
    .circle(RING_OD / 2)
    .extrude(RING_H)
    .faces("<Z")
    .edges()
    .fillet(RING_FIL)
)

# ---------------- arm + hump (side profile extruded across width) ----------------
xs = 0.0  # arm starts at the ring centre (hidden inside the ring)
prof = [
    (xs, ARM_Z0),
    (ARM_END, ARM_Z0),
    (ARM_END, HUMP_Z),
    (HUMP_X0, HUMP_Z),
    (HUMP_X0, ARM_Z1),
    (xs, ARM_Z1),
]
arm0 = (
    cq.Workplane("XZ", origin=(0, ARM_W / 2, 0))
    .polyline(prof)
    .close()
    .extrude(ARM_W)
    .val()
)
hw = ARM_W / 2
xm_h = (HUMP_X0 + ARM_END) / 2
xm_n = (xs + HUMP_X0) / 2
xm_a = (xs + ARM_END) / 2
zm_s = (ARM_Z1 + HUMP_Z) / 2
arm = multi_fillet(
    arm0,
    [
        ((xm_h, hw, HUMP_Z), HUMP_FIL),
        ((xm_h, -hw, HUMP_Z), HUMP_FIL),
        ((HUMP_X0, 0, HUMP_Z), HUMP_FIL),
        ((HUMP_X0, hw, zm_s), HUMP_VFIL),
        ((HUMP_X0, -hw, zm_s), HUMP_VFIL),
        ((HUMP_X0, 0, ARM_Z1), STEP_FIL),
        ((xm_n, hw, ARM_Z1), NECK_TOP_FIL),
        ((xm_n, -hw, ARM_Z1), NECK_TOP_FIL),
        ((xm_a, hw, ARM_Z0), ARM_BOT_FIL),
        ((xm_a, -hw, ARM_Z0), ARM_BOT_FIL),
    ],
)

body = ring.union(cq.Workplane().add(arm))

# ---------------- slope cut across the hump ----------------
cut_prof = [
    (SLOPE_X0, HUMP_Z),
    (SLOPE_X1, ARM_Z1),
    (ARM_END + 10, ARM_Z1),
    (ARM_END + 10, HUMP_Z + 10),
    (SLOPE_X0 - (10 / slope), HUMP_Z + 10),
]
slope_cut = (
    cq.Workplane("XZ", origin=(0, ARM_W, 0))
    .polyline(cut_prof)
    .close()
    .extrude(ARM_W * 2)
)
body = body.cut(slope_cut)

# ---------------- stepped bore ----------------
bore = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .circle(BORE2_D / 2)
    .extrude(RING_H + 2.0)
    .union(
        cq.Workplane("XY", origin=(0, 0, BORE2_H))
        .circle(RING_ID / 2)
        .extrude(RING_H)
    )
)
body = body.cut(bore)

# ---------------- holes & bosses ----------------
n = cq.Vector(nx, 0, nz)
for hx in HOLE_X:
    top = cq.Vector(hx, 0, z_slope(hx))
    bottom_c = top - n * BOSS_DEPTH
    # boss: cylinder from boss face up into the arm
    boss = cq.Solid.makeCylinder(BOSS_D / 2, 25.0, bottom_c, n)
    # recess: everything below boss face inside cylinder
    recess = cq.Solid.makeCylinder(BOSS_D / 2, 40.0, bottom_c, -n)
    body = body.union(cq.Workplane().add(boss)).cut(cq.Workplane().add(recess))
    hole = cq.Solid.makeCylinder(HOLE_D / 2, 120.0, top + n * 30, -n)
    body = body.cut(cq.Workplane().add(hole))

result = body
